import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
OD = 100.0              # outer diameter
H = 50.0                # overall height

# top end: flat rim + countersink down to the thread root
TOP_RIM_R = 47.0        # inner edge of the flat top rim
CSK_ANGLE = 32.0        # countersink cone angle from horizontal (deg)

# internal buttress-style thread (helical)
ROOT_R = 40.3           # thread root radius
CREST_R = 36.85         # thread crest radius (= smallest bore)
PITCH = 4.15
UPPER_FLANK = 0.95      # axial length of the shallow (upper) flank
CREST_FLAT = 1.44       # axial length of the cylindrical crest
LOWER_FLANK = 1.6       # axial length of the steep (lower) flank
Z_THREAD_END = 28.0     # lower end of the threaded zone / outer parting line
THREAD_PHASE = 35.3     # rotation of the helix start about Z (deg)
Z_THREAD_TOP = 45.0     # thread ridge is faced off flat at this height

# plain bore below the thread with two seal grooves
GROOVE_R = 38.1         # groove bottom radius
GROOVES = [(14.3, 17.0), (24.05, 26.65)]   # (lower z, upper z) of each groove

# bottom lead-in cone + flat bottom rim
BOT_RIM_R = 47.2        # inner edge of the flat bottom rim
Z_CONE_TOP = 7.0        # height where the lead-in cone meets the bore

R = OD / 2.0
t = math.tan(math.radians(CSK_ANGLE))
D = ROOT_R - CREST_R
z_csk_bot = H - (TOP_RIM_R - ROOT_R) * t   # countersink meets the root bore


def revolve_profile(pts):
    """Revolve a closed (r, z) polyline about the Z axis."""
    return (
        cq.Workplane("XZ")
        .polyline(pts)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
    )


def ring_void(r, z0, z1):
    """Solid disc r < r, z0 < z < z1 (used as a cutting tool)."""
    return revolve_profile([(0.0, z0), (r, z0), (r, z1), (0.0, z1)])


def n_solids(wp):
    return len(wp.solids().vals())


# ---------------- lower half: bottom rim, lead-in cone, plain bore ----------------
lower = revolve_profile([
    (BOT_RIM_R, 0.0),
    (R, 0.0),
    (R, Z_THREAD_END),
    (CREST_R, Z_THREAD_END),
    (CREST_R, Z_CONE_TOP),
])
for gz0, gz1 in GROOVES:
    lower = lower.cut(ring_void(GROOVE_R, gz0, gz1))

# ---------------- upper half: countersink + internal thread ----------------
csk_void = revolve_profile([
    (0.0, Z_THREAD_TOP),
    (ROOT_R, Z_THREAD_TOP),
    (ROOT_R, z_csk_bot),
    (TOP_RIM_R, H),
    (TOP_RIM_R, H + 2.0),
    (0.0, H + 2.0),
])


def threaded_upper_helical():
    """Upper sleeve with a swept helical buttress thread ridge."""
    sleeve = revolve_profile([
        (ROOT_R, Z_THREAD_END),
        (R, Z_THREAD_END),
        (R, H),
        (ROOT_R, H),
    ])
    ov = 0.15                             # ridge base buried in the wall
    z_start = Z_THREAD_END - 1.0
    z_stop = H - 1.0
    helix = cq.Wire.makeHelix(PITCH, z_stop - z_start, ROOT_R)
    ridge = (
        cq.Workplane("XZ")
        .polyline([
            (CREST_R, 0.0),
            (ROOT_R + ov, UPPER_FLANK * (1 + ov / D)),
            (ROOT_R + ov, -CREST_FLAT - LOWER_FLANK * (1 + ov / D)),
            (CREST_R, -CREST_FLAT),
        ])
        .close()
        .sweep(cq.Workplane("XY").add(helix), isFrenet=True)
        .translate((0, 0, z_start))
        .rotate((0, 0, 0), (0, 0, 1), THREAD_PHASE)
    )
    trim = ring_void(R - 1.0, z_start - 6.0, Z_THREAD_END)
    return sleeve.union(ridge).cut(csk_void).cut(trim)


def threaded_upper_rings():
    """Fallback: the same thread profile as stacked revolved rings."""
    pts = [(R, Z_THREAD_END), (R, H), (TOP_RIM_R, H),
           (ROOT_R, z_csk_bot), (ROOT_R, Z_THREAD_TOP)]
    z = Z_THREAD_TOP
    # walk down: root -> upper flank -> crest -> lower flank -> root
    while z - PITCH > Z_THREAD_END:
        pts += [
            (CREST_R, z - UPPER_FLANK),
            (CREST_R, z - UPPER_FLANK - CREST_FLAT),
            (ROOT_R, z - PITCH),
        ]
        z -= PITCH
    pts += [(ROOT_R, Z_THREAD_END)]
    return revolve_profile(pts)


def plain_upper_volume():
    """Volume of the upper half without any thread ridge (for sanity checks)."""
    return revolve_profile([
        (R, Z_THREAD_END), (R, H), (TOP_RIM_R, H),
        (ROOT_R, z_csk_bot), (ROOT_R, Z_THREAD_END),
    ]).val().Volume()


upper = None
try:
    cand = threaded_upper_helical()
    gained = cand.val().Volume() - plain_upper_volume()
    if n_solids(cand) == 1 and cand.val().isValid() and gained > 2000.0:
        upper = cand
except Exception:
    upper = None
if upper is None:
    upper = threaded_upper_rings()

# join the halves; keep the circumferential parting line at Z_THREAD_END
body = upper.union(lower, clean=False)
if n_solids(body) != 1 or not body.val().isValid():
    body = upper.union(lower)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
